"""Chain of three double split rings (flat flexure / link strip).

Each unit is an outer and an inner C-ring, both opened towards -X.
Neighbouring units are joined by two parallel bars that run from the
outer ring of unit i (which is slotted between the bars) through the
C-opening of unit i+1 into the bore of its inner ring.  The result is
four separate bodies lying in one plane, extruded to a constant
thickness with sharp edges.
"""
import math
import cadquery as cq
from OCP.BRepFeat import BRepFeat_SplitShape

# --- driving dimensions (mm) ---
W = 5.0                 # base strip width (grid unit)
T = 10.0                # plate thickness
N_UNITS = 3             # number of ring pairs in the chain
PITCH = 12 * W          # centre distance between ring pairs
R_IN_I = 3 * W          # inner ring, inner radius (bore)
R_IN_O = 4 * W          # inner ring, outer radius
R_OUT_I = 5 * W         # outer ring, inner radius
R_OUT_O = 6 * W         # outer ring, outer radius
OPEN_OUT = 2.5 * W      # half-height of the outer ring opening (towards -X)
OPEN_IN = 1.5 * W       # half-height of the inner ring opening (towards -X)
SLOT = 0.5 * W          # half-width of the slot between the two link bars
BAR_O = OPEN_IN         # outer edge |y| of the link bars
SEAM = True             # keep the sketch seam of the -Y link bar (cosmetic)

BIG = 100 * W


def ring(cx, r_i, r_o):
    return (cq.Workplane("XY").center(cx, 0)
            .circle(r_o).circle(r_i).extrude(T))


def box(x0, x1, y0, y1):
    return (cq.Workplane("XY")
            .center((x0 + x1) / 2, (y0 + y1) / 2)
            .rect(x1 - x0, y1 - y0).extrude(T))


def bore(cx):
    return cq.Workplane("XY").center(cx, 0).circle(R_IN_I).extrude(T)


# ---- ring pairs ----
result = None
for i in range(N_UNITS):
    cx = i * PITCH
    outer = ring(cx, R_OUT_I, R_OUT_O)
    inner = ring(cx, R_IN_I, R_IN_O)
    # C-openings of both rings towards -X
    outer = outer.cut(box(cx - BIG, cx, -OPEN_OUT, OPEN_OUT))
    inner = inner.cut(box(cx - BIG, cx, -OPEN_IN, OPEN_IN))
    # slot through the outer ring towards the next unit
    if i < N_UNITS - 1:
        outer = outer.cut(box(cx, cx + BIG, -SLOT, SLOT))
    unit = outer.union(inner)
    result = unit if result is None else result.union(unit)

# ---- link bars: outer ring of unit i -> bore of unit i+1 ----
for i in range(N_UNITS - 1):
    cx = i * PITCH
    x0 = cx + 0.5 * (R_OUT_I + R_OUT_O)     # starts inside the outer ring
    x1 = cx + PITCH                         # runs into the next bore
    for s in (1, -1):
        y0, y1 = sorted((s * SLOT, s * BAR_O))
        bar = box(x0, x1, y0, y1).cut(bore(cx + PITCH))
        result = result.union(bar)

# ---- cosmetic seam: the -Y bar face stays split from the inner ring face ----
if SEAM:
    new_solids = []
    for so in result.solids().vals():
        splitter = BRepFeat_SplitShape(so.wrapped)
        added = False
        for i in range(1, N_UNITS):
            cx = i * PITCH
            y = -BAR_O
            xa = cx - math.sqrt(R_IN_O ** 2 - y ** 2)
            xb = cx - math.sqrt(R_IN_I ** 2 - y ** 2)
            for z in (0.0, T):
                probe = cq.Vertex.makeVertex((xa + xb) / 2, y + 1e-3 * W, z)
                for f in so.Faces():
                    if f.geomType() != "PLANE" or abs(f.Center().z - z) > 1e-6:
                        continue
                    if f.distance(probe) > 1e-6:
                        continue
                    e = cq.Edge.makeLine(cq.Vector(xa, y, z), cq.Vector(xb, y, z))
                    splitter.Add(e.wrapped, f.wrapped)
                    added = True
        if added:
            splitter.Build()
            new_solids.append(cq.Shape.cast(splitter.Shape()))
        else:
            new_solids.append(so)
    result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(new_solids)])

VIEW = {"azimuth": 45, "elevation": 26}
